import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BAR_W = 24.8          # bar width (= diameter of the rounded ends)
BAR_T = 7.0           # bar (plate) thickness
CC = 175.3            # centre-to-centre distance of the two conical bosses
CONE_D0 = 20.8        # cone base diameter (on top of the bar)
CONE_D1 = 9.5         # cone top diameter (flat top)
CONE_H = 20.7         # cone height above the bar top face
HOLE_D = 4.0          # through hole (cone top to bar underside)
ANGLE = 7.32          # rotation of the bar axis about Z, from +Y towards -X (deg)

# cosmetic: angle (in the final part) at which the cone's parametric seam sits,
# chosen so it lies on a silhouette in the standard views
SEAM_DIR = 45.0

# ---------------- bar: stadium plate along local Y ----------------
bar = (
    cq.Workplane("XY")
    .slot2D(CC + BAR_W, BAR_W, angle=90)
    .extrude(BAR_T)
)

# ---------------- conical bosses at both ends ----------------
boss_pts = [(0.0, -CC / 2.0), (0.0, CC / 2.0)]


def cone_at(x, y):
    c = cq.Solid.makeCone(
        CONE_D0 / 2.0, CONE_D1 / 2.0, CONE_H,
        pnt=cq.Vector(0, 0, BAR_T), dir=cq.Vector(0, 0, 1),
    )
    # spin about its own axis (only moves the seam), then place it
    c = c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_DIR - ANGLE)
    return c.translate(cq.Vector(x, y, 0))


part = bar
for (x, y) in boss_pts:
    part = part.union(cq.Workplane("XY").add(cone_at(x, y)))

# ---------------- through holes on the boss axes ----------------
holes = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .pushPoints(boss_pts)
    .circle(HOLE_D / 2.0)
    .extrude(BAR_T + CONE_H + 2.0)
)
part = part.cut(holes)

# ---------------- final orientation ----------------
result = part.rotate((0, 0, 0), (0, 0, 1), ANGLE)

VIEW = {"azimuth": 45, "elevation": 26}
